import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
K = 0.4                      # scale factor (reference units -> mm)

R0 = 98.6 * K                # outer radius at the open front end
LF = 146.0 * K               # length of the front (large) section
RMID = 86.25 * K             # front section radius half way along (convex arc)
RFE = 70.14 * K              # outer radius at the end of the front section
RB0 = 80.3 * K               # collar radius at start of back cone
RB1 = 55.0 * K               # radius at the back end
LB = 90.8 * K                # length of back cone
L = LF + LB                  # overall length

# interior
RBORE1 = 87.6 * K            # front counterbore radius
D1 = 32.0 * K                # front counterbore depth
RBORE2 = 77.0 * K            # bore radius right after the ledge
YFLOOR = 109.0 * K           # axial position of the cavity floor
RCAV_END = 65.4 * K          # cavity radius at floor
FLOOR_FILLET = 0.0           # rounding between cavity wall and floor
RFLOOR_HOLE = 35.4 * K       # aperture through the cavity floor
RBACK = 38.4 * K             # bore of the back section
RBACK_CB = 43.0 * K          # counterbore at the back end
BACK_CB_D = 1.5              # counterbore depth

# front rim recesses (4x) with radial holes
TAB_W = 20.4 * K
TAB_L = 30.8 * K
TAB_FLOOR = 89.5 * K
TAB_HOLE_D = 11.0 * K
TAB_HOLE_Y = 20.6 * K

# bayonet pockets at rear of front cone (4x, 45 deg each)
WIN_Y0 = 120.6 * K
WIN_SPAN = 45.0
WIN_FLOOR = RFE - 3.0         # pocket floor (concentric cylinder)

# vertical hole on top that opens into a wide funnel (scoop)
FUN_Z0 = 22.0                # funnel bottom height (meets the hole)
FUN_Z1 = 40.0                # funnel top plane (above the part)
FUN_X_HALF = 13.1            # footprint half width on the skin ...
FUN_X_Z = 31.64              # ... at this height
FUN_FRONT_Y = 20.6           # footprint front edge on the skin ...
FUN_FRONT_Z = 36.11          # ... at this height
FUN_BACK_Y = 40.44           # footprint back edge on the skin ...
FUN_BACK_Z = 32.2            # ... at this height
SCOOP_HOLE_R = 14.5 * K
SCOOP_HOLE_Y = 71.8 * K

# internal boss under the scoop
BOSS_HW = 31.2 * K
BOSS_ZB = 44.7 * K
BOSS_Y0 = 43.75 * K
BOSS_FRAME = 4.8             # rim left around the pocket under the boss
BOSS_POCKET_D = 1.5          # pocket depth
BOSS_PIN_D = 1.6             # small corner holes in the rim
BOSS_PIN_INSET = 3.3         # pin hole centre distance from the boss edges
BOSS_PIN_DEPTH = 4.0

OUTER_SEAM_ROT = 135.0       # park revolve seams where they are least visible
CAVITY_SEAM_ROT = -90.0


def revolve_profile(pts):
    """Revolve an (r, y) profile 360 deg about the Y axis."""
    return (cq.Workplane("XY").polyline(pts).close()
            .revolve(360, (0, 0, 0), (0, 1, 0)))


# ---------------- main body ----------------
outer = (cq.Workplane("XY")
         .moveTo(0, 0).lineTo(R0, 0)
         .spline([(RMID, LF / 2), (RFE, LF)], includeCurrent=True)
         .lineTo(RB0, LF).lineTo(RB1, L).lineTo(0, L).close()
         .revolve(360, (0, 0, 0), (0, 1, 0))
         .rotate((0, 0, 0), (0, 1, 0), OUTER_SEAM_ROT))

def fillet_corner(p_prev, p, p_next, rf):
    """Tangent points and arc mid point for rounding the corner p."""
    ax, ay = p_prev[0] - p[0], p_prev[1] - p[1]
    bx, by = p_next[0] - p[0], p_next[1] - p[1]
    la, lb = math.hypot(ax, ay), math.hypot(bx, by)
    ax, ay, bx, by = ax / la, ay / la, bx / lb, by / lb
    th = math.acos(max(-1.0, min(1.0, ax * bx + ay * by)))
    t = rf / math.tan(th / 2)
    t1 = (p[0] + ax * t, p[1] + ay * t)
    t2 = (p[0] + bx * t, p[1] + by * t)
    mx, my = ax + bx, ay + by
    lm = math.hypot(mx, my)
    d = rf / math.sin(th / 2) - rf
    mid = (p[0] + mx / lm * d, p[1] + my / lm * d)
    return t1, mid, t2


p_led = (RBORE2, D1)
p_cor = (RCAV_END, YFLOOR)
p_flr = (RFLOOR_HOLE, YFLOOR)
cav = (cq.Workplane("XY")
       .moveTo(0, -1).lineTo(RBORE1, -1).lineTo(RBORE1, D1).lineTo(*p_led))
if FLOOR_FILLET > 0:
    ft1, fmid, ft2 = fillet_corner(p_led, p_cor, p_flr, FLOOR_FILLET)
    cav = cav.lineTo(*ft1).threePointArc(fmid, ft2)
else:
    cav = cav.lineTo(*p_cor)
cavity = (cav
          .lineTo(*p_flr).lineTo(RFLOOR_HOLE, LF)
          .lineTo(RBACK, LF).lineTo(RBACK, L - BACK_CB_D)
          .lineTo(RBACK_CB, L - BACK_CB_D).lineTo(RBACK_CB, L + 1)
          .lineTo(0, L + 1).close()
          .revolve(360, (0, 0, 0), (0, 1, 0))
          .rotate((0, 0, 0), (0, 1, 0), CAVITY_SEAM_ROT))

body = outer.cut(cavity)

# internal boss (clipped to the cavity so it never pokes through)
cav_clip = revolve_profile([
    (0, D1), (RBORE2 + 1, D1), (RCAV_END + 1, YFLOOR + 0.01), (0, YFLOOR + 0.01)
])
boss = (cq.Workplane("XY")
        .box(2 * BOSS_HW, YFLOOR - BOSS_Y0 + 1, 40, centered=(True, False, False))
        .translate((0, BOSS_Y0, BOSS_ZB))
        .intersect(cav_clip))
body = body.union(boss)

# shallow pocket in the underside of the boss, leaving a rim with small holes
pocket = (cq.Workplane("XY")
          .box(2 * (BOSS_HW - BOSS_FRAME), YFLOOR - BOSS_Y0 - 2 * BOSS_FRAME,
               BOSS_POCKET_D + 1, centered=(True, False, False))
          .translate((0, BOSS_Y0 + BOSS_FRAME, BOSS_ZB - 1)))
body = body.cut(pocket)
pin_pts = [(sx * (BOSS_HW - BOSS_PIN_INSET), yy)
           for sx in (-1, 1)
           for yy in (BOSS_Y0 + BOSS_PIN_INSET, YFLOOR - BOSS_PIN_INSET)]
pins = (cq.Workplane("XY").workplane(offset=BOSS_ZB - 1)
        .pushPoints(pin_pts).circle(BOSS_PIN_D / 2).extrude(BOSS_PIN_DEPTH + 1))
body = body.cut(pins)

# ---------------- front rim recesses with radial holes ----------------
for k in range(4):
    phi = k * 90.0
    rec = (cq.Workplane("XY")
           .box(TAB_W, TAB_L + 1, 20, centered=(True, False, False))
           .translate((0, -1, TAB_FLOOR))
           .rotate((0, 0, 0), (0, 1, 0), phi))
    hole = (cq.Workplane("XY")
            .circle(TAB_HOLE_D / 2).extrude(20)
            .translate((0, TAB_HOLE_Y, TAB_FLOOR - 8))
            .rotate((0, 0, 0), (0, 1, 0), phi))
    body = body.cut(rec).cut(hole)

# ---------------- bayonet pockets ----------------
for k in range(4):
    sector = (cq.Workplane("XY")
              .polyline([(WIN_FLOOR, WIN_Y0), (R0 + 5, WIN_Y0),
                         (R0 + 5, LF), (WIN_FLOOR, LF)]).close()
              .revolve(WIN_SPAN, (0, 0, 0), (0, 1, 0)))
    # sector spans phi in [90, 90+span]; move to [k*90-45, k*90]
    sector = sector.rotate((0, 0, 0), (0, 1, 0), k * 90.0 - WIN_SPAN - 90.0)
    body = body.cut(sector)

# ---------------- hole on top opening into a deep funnel ----------------
# ruled loft from the hole circle (at depth) to an ellipse above the part; the
# ellipse is sized so the funnel meets the outer skin on the measured footprint
def funnel_top(z0, z1):
    sx = (FUN_X_Z - z0) / (z1 - z0)
    sf = (FUN_FRONT_Z - z0) / (z1 - z0)
    sb = (FUN_BACK_Z - z0) / (z1 - z0)
    a = SCOOP_HOLE_R + (FUN_X_HALF - SCOOP_HOLE_R) / sx
    y_lo = (SCOOP_HOLE_Y - SCOOP_HOLE_R) + (FUN_FRONT_Y - (SCOOP_HOLE_Y - SCOOP_HOLE_R)) / sf
    y_hi = (SCOOP_HOLE_Y + SCOOP_HOLE_R) + (FUN_BACK_Y - (SCOOP_HOLE_Y + SCOOP_HOLE_R)) / sb
    return a, (y_lo + y_hi) / 2, (y_hi - y_lo) / 2


fa, fyc, fb = funnel_top(FUN_Z0, FUN_Z1)
funnel = (cq.Workplane("XY").workplane(offset=FUN_Z0)
          .center(0, SCOOP_HOLE_Y).circle(SCOOP_HOLE_R)
          .workplane(offset=FUN_Z1 - FUN_Z0)
          .center(0, fyc - SCOOP_HOLE_Y).ellipse(fa, fb)
          .loft(ruled=True))
shole = (cq.Workplane("XY").workplane(offset=BOSS_ZB - 1)
         .center(0, SCOOP_HOLE_Y).circle(SCOOP_HOLE_R)
         .extrude(FUN_Z0 - BOSS_ZB + 1.5))
body = body.cut(funnel).cut(shole)

result = body
